import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
N_ARMS = 6            # six-way cross
ARM0_DEG = 90.0       # first arm points along +Y
R_TIP = 300.0         # radius to the prong tips
NOTCH_W = 52.8        # width of the slot between the two prongs
PRONG_W = 17.6        # width of each prong
NOTCH_BOTTOM = 201.5  # radius to the bottom of the slot
NOSE_R = 28.0         # radius of the convex nose at each prong tip
ARC_D = 304.0         # distance from centre to the centre of the big concave arcs
THK = 6.5             # plate thickness
PITCH_Z = 72.4        # vertical pitch between the two stacked plates
N_PLATES = 2

HOLE_D = 6.0
PRONG_HOLE_OFF = 32.8                 # hole line offset from the arm axis
PRONG_HOLE_X = [209.0, 246.0, 283.0]  # radial positions of prong holes
BASE_HOLE_X = 195.0                   # radial position of holes below the slot
BASE_HOLE_OFF = 19.0                  # their offset from the arm axis

# ---------------- derived ----------------
HW = NOTCH_W / 2.0
A = HW + PRONG_W                       # half width of the arm over the prongs
HALF = math.pi / N_ARMS                # half the angle between arms
ARC_R = ARC_D * math.sin(HALF) - A     # big arc tangent to the prong outer edge line
XT = ARC_D * math.cos(HALF)            # that tangent point, along the arm axis
DN = math.sqrt(NOSE_R ** 2 - (NOSE_R - PRONG_W) ** 2)  # nose length along the arm


def rot(p, ang):
    c, s = math.cos(ang), math.sin(ang)
    return (p[0] * c - p[1] * s, p[0] * s + p[1] * c)


def half_gap_samples():
    """Points + unit tangents (arm frame, left prong, y>0) of the smooth flank
    running from the inner tip corner of the prong to the apex of the concave
    arc between two arms.  Nose arc -> short straight -> big concave arc."""
    pts = []
    # nose arc (centre below the outer edge line)
    cx, cy = R_TIP - DN, A - NOSE_R
    a0 = math.atan2(HW - cy, R_TIP - cx)
    a1 = math.pi / 2
    for t in (0.0, 0.5, 1.0):
        a = a0 + (a1 - a0) * t
        p = (cx + NOSE_R * math.cos(a), cy + NOSE_R * math.sin(a))
        tg = (-math.sin(a), math.cos(a))          # CCW on the nose
        pts.append((p, tg))
    # short straight run along the outer edge of the prong
    for t in (0.5,):
        pts.append((((R_TIP - DN) + (XT - (R_TIP - DN)) * t, A), (-1.0, 0.0)))
    # big concave arc, centre at ARC_D along the gap bisector
    bx, by = ARC_D * math.cos(HALF), ARC_D * math.sin(HALF)
    b0 = math.atan2(A - by, XT - bx)               # tangent point (-90 deg)
    b1 = HALF - math.pi                            # apex direction from centre
    for t in (0.0, 1.0 / 3.0, 2.0 / 3.0, 1.0):
        b = b0 + (b1 - b0) * t
        p = (bx + ARC_R * math.cos(b), by + ARC_R * math.sin(b))
        tg = (math.sin(b), -math.cos(b))           # clockwise about the arc centre
        pts.append((p, tg))
    return pts


def outline():
    """Closed outline of one plate as a list of edges."""
    half = half_gap_samples()
    edges = []
    V = cq.Vector
    for i in range(N_ARMS):
        phi = math.radians(ARM0_DEG) + i * 2 * HALF
        # slot of arm i: right tip corner -> slot bottom -> left tip corner
        q1 = rot((R_TIP, -HW), phi)
        q2 = rot((NOTCH_BOTTOM, -HW), phi)
        q3 = rot((NOTCH_BOTTOM, HW), phi)
        q4 = rot((R_TIP, HW), phi)
        edges.append(cq.Edge.makeLine(V(*q1, 0), V(*q2, 0)))
        edges.append(cq.Edge.makeLine(V(*q2, 0), V(*q3, 0)))
        edges.append(cq.Edge.makeLine(V(*q3, 0), V(*q4, 0)))
        # flank from left tip of arm i to the right tip of arm i+1 (one spline)
        pts, tgs = [], []
        for p, t in half:
            pts.append(rot(p, phi))
            tgs.append(rot(t, phi))
        # mirrored half, reflected about the gap bisector, reversed
        mirror = []
        for p, t in reversed(half[:-1]):
            pm = (p[0], -p[1])
            tm = (-t[0], t[1])
            ang = phi + 2 * HALF
            mirror.append((rot(pm, ang), rot(tm, ang)))
        for p, t in mirror:
            pts.append(p)
            tgs.append(t)
        edges.append(cq.Edge.makeSpline([V(*p, 0) for p in pts],
                                        tangents=[V(*t, 0) for t in tgs]))
    return edges


def plate():
    wire = cq.Wire.assembleEdges(outline())
    face = cq.Face.makeFromWires(wire)
    body = cq.Workplane("XY").add(cq.Solid.extrudeLinear(face, cq.Vector(0, 0, THK)))

    pts = []
    for i in range(N_ARMS):
        phi = math.radians(ARM0_DEG) + i * 2 * HALF
        for x in PRONG_HOLE_X:
            for sgn in (-1, 1):
                pts.append(rot((x, sgn * PRONG_HOLE_OFF), phi))
        for sgn in (-1, 1):
            pts.append(rot((BASE_HOLE_X, sgn * BASE_HOLE_OFF), phi))
    holes = (cq.Workplane("XY").pushPoints(pts).circle(HOLE_D / 2.0)
             .extrude(THK * 3).translate((0, 0, -THK)))
    return body.cut(holes)


single = plate()
result = single
for k in range(1, N_PLATES):
    result = result.union(single.translate((0, 0, k * PITCH_Z)))

VIEW = {"azimuth": 45, "elevation": 26}
